import cadquery as cq

# =====================================================================
#  Peg plate: flat rectangular plate (XZ plane) with 6 mm cube pegs on
#  the front face (-Y side) and a set of through holes (component
#  mounting pattern).  Perimeter pegs sit flush with the plate edges.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
W = 207.0          # plate width  (X)
H = 237.0          # plate height (Z)
T = 3.5            # plate thickness (Y)
B = 6.0            # cube peg size in the plate plane (X, Z)
BD = 6.0           # peg protrusion from the front face (toward -Y)
PX = 50.25         # peg column pitch  (W/2 - B/2 = 2*PX)
PZ = 38.5          # peg row pitch     (H/2 - B/2 = 3*PZ)
D_MED = 5.5        # medium through-hole diameter
D_SML = 2.75       # small through-hole diameter
R_BASE = 0.5       # small concave fillet where the pegs meet the plate face
C_FRONT = 0.5      # small chamfer on the front-face perimeter edges of the plate

# ---------------- plate ----------------
# plate occupies y in [0, T]; front face at y = 0, pegs protrude to -Y
plate = cq.Workplane("XZ").rect(W, H).extrude(-T)

# ---------------- peg layout ----------------
ex = W / 2 - B / 2          # x of pegs flush with the left / right edges
ez = H / 2 - B / 2          # z of pegs flush with the top / bottom edges
cols = [-ex, -PX, 0.0, PX, ex]                     # 5 columns
rows = [ez, 2 * PZ, PZ, 0.0, -PZ, -2 * PZ, -ez]    # 7 rows

pegs = set()
for c in cols:                       # top & bottom edge pegs
    pegs.add((c, ez))
    pegs.add((c, -ez))
for r in rows:                       # left & right edge pegs
    pegs.add((-ex, r))
    pegs.add((ex, r))
for r in [2 * PZ, 0.0, -PZ, -2 * PZ]:   # regular interior grid
    for c in [-PX, 0.0, PX]:
        pegs.add((c, r))
for c in [-PX, 0.5 * PX, 1.5 * PX]:     # row PZ: two pegs shifted half a pitch
    pegs.add((c, PZ))
pegs = sorted((round(x, 4), round(z, 4)) for x, z in pegs)

peg_solids = (
    cq.Workplane("XZ")
    .pushPoints(pegs)
    .rect(B, B)
    .extrude(BD)             # XZ normal is -Y -> pegs grow toward -Y
)
body = plate.union(peg_solids)

# concave fillet at the foot of every peg: edges lying in the front-face
# plane (y = 0) that are not part of the plate's outer perimeter
def _is_peg_foot(e, tol=1e-3):
    a, b = e.startPoint(), e.endPoint()
    if abs(a.y) > tol or abs(b.y) > tol:
        return False
    if abs(a.x - b.x) < tol and abs(abs(a.x) - W / 2) < tol:
        return False
    if abs(a.z - b.z) < tol and abs(abs(a.z) - H / 2) < tol:
        return False
    return True

if R_BASE > 0:
    foot = [e for e in body.edges().vals() if _is_peg_foot(e)]
    body = body.newObject(foot).fillet(R_BASE)

# small chamfer on the plate's front-face perimeter (between the edge pegs)
def _is_front_perimeter(e, tol=1e-3):
    a, b = e.startPoint(), e.endPoint()
    if abs(a.y) > tol or abs(b.y) > tol:
        return False
    if abs(a.x - b.x) < tol and abs(abs(a.x) - W / 2) < tol:
        return True
    if abs(a.z - b.z) < tol and abs(abs(a.z) - H / 2) < tol:
        return True
    return False

if C_FRONT > 0:
    rim = [e for e in body.edges().vals() if _is_front_perimeter(e)]
    body = body.newObject(rim).chamfer(C_FRONT)

# ---------------- through holes (x, z) from the plate centre ----------------
med_holes = [
    (-73.05, 99.85), (-70.15, 85.85), (-70.15, 72.15),      # upper-left trio
    (64.25, 68.65),                                          # upper-right
    (-5.45, 46.05), (6.35, 34.35), (17.95, 22.55),          # diagonal trio
    (-51.45, -84.55), (-54.15, -98.95),                      # lower-left pair
    (47.65, -84.55), (50.15, -98.95),                        # lower-right pair
]
small_holes = [
    (-32.95, 103.65), (-88.95, 49.35), (-32.95, 49.35),
    (29.75, 73.85), (41.45, 73.85), (29.75, 66.95), (41.45, 66.95),  # 2x2
    (50.35, 49.65), (50.35, 38.35), (50.35, 27.55),          # vertical trio
    (-17.55, -0.4), (-21.35, -10.95), (-25.25, -21.2),       # slanted trio
    (-7.85, -44.45), (3.95, -44.45),                         # pair
    (-7.85, -93.85), (3.85, -93.85),                         # pair
]


def hole_cutters(pts, d):
    # cylinders running through the full plate thickness (+ margin)
    return (
        cq.Workplane("XZ", origin=(0, T + 1, 0))
        .pushPoints(pts)
        .circle(d / 2)
        .extrude(T + 2)
    )


body = body.cut(hole_cutters(med_holes, D_MED)).cut(hole_cutters(small_holes, D_SML))

result = body
VIEW = {"azimuth": 45, "elevation": 26}
